import math
import cadquery as cq

# ---------------------------------------------------------------
# Light freighter (diamond-planform hull) - driving dimensions (mm)
# X = span, Y = length (nose at -Y), Z = up
# ---------------------------------------------------------------
Z_WALL_T = 13.5      # top of perimeter wall
Z_WALL_B = 11.3      # bottom of perimeter wall
Z_MID = 0.5 * (Z_WALL_T + Z_WALL_B)
Z_RIDGE_T = 21.0     # upper ridge height (centre body / band)
Z_RIDGE_B = 4.8      # lower ridge height
Y_BAND_F = -13.2     # transverse band front edge
Y_BAND_R = -1.2      # transverse band rear edge
Y_BAND_C = 0.5 * (Y_BAND_F + Y_BAND_R)
X_TIP = 38.3         # wing tip (pod root)
X_C = 15.0           # half width of centre body at band
F_X, F_Y = 14.3, -43.9   # front corner of hull
R_X, R_Y = 15.4, 29.4    # rear corner of hull

BAND_RAISE = 1.0     # band stands proud of hull
Z_KEEL = 0.0         # bottom of keel
KEEL_W = 13.6        # keel half width at bottom
KEEL_Y_R = 37.8      # keel rear end

SPINE_W_R = 7.6      # spine half width at rear
SPINE_W_F = 5.2      # spine half width at front
SPINE_TOP = 25.8
SPINE_Y_F = -38.5

POD_R = 5.0          # pod body half size
POD_X0 = 29.5
POD_X1 = 39.8
POD_TIP = 42.4

ENG_X = 7.8
ENG_Z = 20.4
CEN_Z_MID = 15.2
CEN_Z_LOW = 9.0


def poly_solid(verts, faces):
    """Planar-faceted solid from explicit vertex/face lists."""
    fl = []
    for f in faces:
        w = cq.Wire.makePolygon([cq.Vector(*verts[i]) for i in f], close=True)
        fl.append(cq.Face.makeFromWires(w))
    sh = cq.Shell.makeShell(fl)
    return cq.Solid.makeSolid(sh)


# ---------------- main wing (bi-pyramid diamond hull) ----------------
V = {}
for s, tag in ((1, "R"), (-1, "L")):
    V["Ft" + tag] = (s * F_X, F_Y, Z_WALL_T)
    V["Fb" + tag] = (s * F_X, F_Y, Z_WALL_B)
    V["Tft" + tag] = (s * X_TIP, Y_BAND_F, Z_WALL_T)
    V["Tfb" + tag] = (s * X_TIP, Y_BAND_F, Z_WALL_B)
    V["Trt" + tag] = (s * X_TIP, Y_BAND_R, Z_WALL_T)
    V["Trb" + tag] = (s * X_TIP, Y_BAND_R, Z_WALL_B)
    V["Rt" + tag] = (s * R_X, R_Y, Z_WALL_T)
    V["Rb" + tag] = (s * R_X, R_Y, Z_WALL_B)
    V["Cft" + tag] = (s * X_C, Y_BAND_F, Z_RIDGE_T)
    V["Crt" + tag] = (s * X_C, Y_BAND_R, Z_RIDGE_T)
    V["Cfb" + tag] = (s * X_C, Y_BAND_F, Z_RIDGE_B)
    V["Crb" + tag] = (s * X_C, Y_BAND_R, Z_RIDGE_B)
names = list(V.keys())
idx = {n: i for i, n in enumerate(names)}
verts = [V[n] for n in names]
F = []
for t in ("R", "L"):
    F += [
        ["Ft" + t, "Tft" + t, "Cft" + t],
        ["Tft" + t, "Trt" + t, "Crt" + t, "Cft" + t],
        ["Trt" + t, "Rt" + t, "Crt" + t],
        ["Fb" + t, "Cfb" + t, "Tfb" + t],
        ["Tfb" + t, "Cfb" + t, "Crb" + t, "Trb" + t],
        ["Trb" + t, "Crb" + t, "Rb" + t],
        ["Ft" + t, "Fb" + t, "Tfb" + t, "Tft" + t],
        ["Tft" + t, "Tfb" + t, "Trb" + t, "Trt" + t],
        ["Trt" + t, "Trb" + t, "Rb" + t, "Rt" + t],
    ]
F += [
    ["FtR", "FtL", "CftL", "CftR"],
    ["CftR", "CftL", "CrtL", "CrtR"],
    ["CrtR", "CrtL", "RtL", "RtR"],
    ["FbR", "CfbR", "CfbL", "FbL"],
    ["CfbR", "CrbR", "CrbL", "CfbL"],
    ["CrbR", "RbR", "RbL", "CrbL"],
    ["FtR", "FbR", "FbL", "FtL"],
    ["RtR", "RtL", "RbL", "RbR"],
]
wing = cq.Workplane("XY").add(poly_solid(verts, [[idx[n] for n in f] for f in F]))

# raised triangular panels on the eight quadrant faces
PANEL_INSET = 1.6
PANEL_H = 0.35


def _v(p):
    return cq.Vector(*p)


def raised_poly(pts, n, h):
    """Thin plate raised by h along unit normal n from planar polygon pts."""
    lo = [p - n * 0.15 for p in pts]
    hi = [p + n * h for p in pts]
    k = len(pts)
    vv = [(p.x, p.y, p.z) for p in lo + hi]
    ff = [list(range(k - 1, -1, -1)), list(range(k, 2 * k))]
    for i in range(k):
        j = (i + 1) % k
        ff.append([i, j, k + j, k + i])
    return poly_solid(vv, ff)


def quadrant_panels(p0, p1, p2, up, inset=PANEL_INSET, h=PANEL_H, t1=0.40, t2=0.48):
    """Perimeter edge p0-p1, apex p2: a raised strip along the edge and a
    raised triangle towards the apex, separated by a groove."""
    a, b, c = _v(p0), _v(p1), _v(p2)
    n = (b - a).cross(c - a).normalized()
    if (n.z > 0) != up:
        n = n * -1
    la, lb, lc = (b - c).Length, (c - a).Length, (a - b).Length
    per = la + lb + lc
    inc = (a * la + b * lb + c * lc) * (1.0 / per)
    area = 0.5 * (b - a).cross(c - a).Length
    r_in = 2 * area / per
    k = (r_in - inset) / r_in
    a2, b2, c2 = [inc + (p - inc) * k for p in (a, b, c)]
    strip = [a2, b2, b2 + (c2 - b2) * t1, a2 + (c2 - a2) * t1]
    tri = [a2 + (c2 - a2) * t2, b2 + (c2 - b2) * t2, c2]
    return [raised_poly(strip, n, h), raised_poly(tri, n, h)]


panels = cq.Workplane("XY")
for t in ("R", "L"):
    for sol in (quadrant_panels(V["Ft" + t], V["Tft" + t], V["Cft" + t], True)
                + quadrant_panels(V["Rt" + t], V["Trt" + t], V["Crt" + t], True)):
        panels = panels.add(sol)

# raised panels on the sloping shelf either side of the spine (front half)
def shelf_z(y):
    return Z_WALL_T + (y - F_Y) * (Z_RIDGE_T - Z_WALL_T) / (Y_BAND_F - F_Y)


shelf_n = cq.Vector(0, -(Z_RIDGE_T - Z_WALL_T), (Y_BAND_F - F_Y)).normalized()
for s in (1, -1):
    for (y0, y1, x0, x1) in ((-42.6, -33.5, 7.0, 13.4), (-31.8, -15.0, 7.4, 13.8)):
        pts = [cq.Vector(s * x0, y0, shelf_z(y0)), cq.Vector(s * x1, y0, shelf_z(y0)),
               cq.Vector(s * x1, y1, shelf_z(y1)), cq.Vector(s * x0, y1, shelf_z(y1))]
        if s < 0:
            pts = pts[::-1]
        panels = panels.add(raised_poly(pts, shelf_n, PANEL_H))

# greeble groove running round the diagonal perimeter walls
plan = [(F_X, F_Y), (X_TIP, Y_BAND_F), (X_TIP, Y_BAND_R), (R_X, R_Y),
        (-R_X, R_Y), (-X_TIP, Y_BAND_R), (-X_TIP, Y_BAND_F), (-F_X, F_Y)]
GROOVE_H, GROOVE_D = 1.5, 1.0
g_out = (cq.Workplane("XY").workplane(offset=Z_MID - 0.5 * GROOVE_H)
         .polyline(plan).close().extrude(GROOVE_H))
g_in = (cq.Workplane("XY").workplane(offset=Z_MID - 0.5 * GROOVE_H - 0.1)
        .polyline(plan).close().offset2D(-GROOVE_D).extrude(GROOVE_H + 0.2))
groove = g_out.cut(g_in).cut(
    cq.Workplane("XY").box(2 * (F_X + 1.5), 200, 40).translate((0, 0, Z_MID)))
for p in panels.vals():
    wing = wing.union(cq.Workplane('XY').add(p))
wing = wing.cut(groove)

# ---------------- centre body ----------------
centre = (cq.Workplane("XY").workplane(offset=4.0)
          .polyline([(F_X, F_Y), (R_X, R_Y), (-R_X, R_Y), (-F_X, F_Y)]).close()
          .extrude(Z_WALL_T - 4.0 - 0.3))

# ---------------- transverse bands (upper and lower) ----------------
bt = Z_RIDGE_T + BAND_RAISE
bt_tip = Z_WALL_T + BAND_RAISE
band_up = (cq.Workplane("XZ", origin=(0, Y_BAND_R, 0))
           .polyline([(-X_TIP, Z_MID), (-X_TIP, bt_tip), (-X_C, bt), (X_C, bt),
                      (X_TIP, bt_tip), (X_TIP, Z_MID)]).close()
           .extrude(Y_BAND_R - Y_BAND_F))
bb = Z_RIDGE_B - 1.3
bb_tip = Z_WALL_B - 1.3
band_lo = (cq.Workplane("XZ", origin=(0, Y_BAND_R, 0))
           .polyline([(-X_TIP, Z_MID), (-X_TIP, bb_tip), (-X_C, bb), (X_C, bb),
                      (X_TIP, bb_tip), (X_TIP, Z_MID)]).close()
           .extrude(Y_BAND_R - Y_BAND_F))
# ladder grooves and chevron pockets on both bands
LADDER_X = (18.7, 23.1, 27.0)
CHEV_X0, CHEV_X1 = 26.8, 32.0      # chevron apex / base position
for (band_z0, band_z1, up) in ((bt, bt_tip, True), (bb, bb_tip, False)):
    slope = (band_z1 - band_z0) / (X_TIP - X_C)
    cuts = cq.Workplane("XY")
    for s in (1, -1):
        nrm = cq.Vector(-s * slope, 0, 1).normalized() * (1 if up else -1)

        def zb(x):
            return band_z0 + (x - X_C) * slope
        for gx in LADDER_X:
            pts = [cq.Vector(s * (gx - 0.45), Y_BAND_F + 0.6, zb(gx - 0.45)),
                   cq.Vector(s * (gx + 0.45), Y_BAND_F + 0.6, zb(gx + 0.45)),
                   cq.Vector(s * (gx + 0.45), Y_BAND_R - 0.6, zb(gx + 0.45)),
                   cq.Vector(s * (gx - 0.45), Y_BAND_R - 0.6, zb(gx - 0.45))]
            cuts = cuts.add(raised_poly([p - nrm * 0.45 for p in pts], nrm, 1.5))
        tri = [cq.Vector(s * CHEV_X0, Y_BAND_C, zb(CHEV_X0)),
               cq.Vector(s * CHEV_X1, Y_BAND_F + 1.3, zb(CHEV_X1)),
               cq.Vector(s * CHEV_X1, Y_BAND_R - 1.3, zb(CHEV_X1))]
        cuts = cuts.add(raised_poly([p - nrm * 0.5 for p in tri], nrm, 1.5))
    for c in cuts.vals():
        if up:
            band_up = band_up.cut(cq.Workplane("XY").add(c))
        else:
            band_lo = band_lo.cut(cq.Workplane("XY").add(c))

# ---------------- keel ----------------
KEEL_W_R = 4.0       # keel half width at its rear end
keel_side = (cq.Workplane("YZ", origin=(-KEEL_W - 2, 0, 0))
             .polyline([(Y_BAND_F + 0.4, Z_KEEL), (0.0, Z_KEEL), (KEEL_Y_R, 3.6),
                        (KEEL_Y_R, 5.5), (Y_BAND_F + 0.4, 5.5)]).close()
             .extrude(2 * (KEEL_W + 2)))
keel_plan = (cq.Workplane("XY").workplane(offset=-1.0)
             .polyline([(-KEEL_W - 1.4, Y_BAND_F + 0.4), (KEEL_W + 1.4, Y_BAND_F + 0.4),
                        (KEEL_W_R + 1.4, KEEL_Y_R), (-KEEL_W_R - 1.4, KEEL_Y_R)]).close()
             .extrude(14.0))
keel = keel_side.intersect(keel_plan)
# chamfer the lower long edges by intersecting with a tapered-plan copy
keel_low = (cq.Workplane("XY").workplane(offset=-1.0)
            .polyline([(-KEEL_W, Y_BAND_F + 0.4), (KEEL_W, Y_BAND_F + 0.4),
                       (KEEL_W_R, KEEL_Y_R), (-KEEL_W_R, KEEL_Y_R)]).close()
            .extrude(5.0))
keel_up = (cq.Workplane("XY").workplane(offset=2.5)
           .polyline([(-KEEL_W - 1.4, Y_BAND_F + 0.4), (KEEL_W + 1.4, Y_BAND_F + 0.4),
                      (KEEL_W_R + 1.4, KEEL_Y_R), (-KEEL_W_R - 1.4, KEEL_Y_R)]).close()
           .extrude(12.0))
keel = keel.intersect(keel_low.union(keel_up))

# rear lower block (engine mount)
REAR_BLK_W = 4.0
rear_block = (cq.Workplane("YZ", origin=(-REAR_BLK_W, 0, 0))
              .polyline([(24.0, 3.0), (KEEL_Y_R, 3.6), (KEEL_Y_R, 13.2), (24.0, 13.2)])
              .close().extrude(2 * REAR_BLK_W))

# ---------------- spine ----------------
SPINE_Y_RS = 15.0     # start of the raised rear deck section
spine_plan = (cq.Workplane("XY").workplane(offset=10.0)
              .polyline([(-SPINE_W_F, SPINE_Y_F), (SPINE_W_F, SPINE_Y_F),
                         (SPINE_W_R, SPINE_Y_RS + 3.0), (-SPINE_W_R, SPINE_Y_RS + 3.0)]).close()
              .extrude(20.0))
spine_side = (cq.Workplane("YZ", origin=(-20, 0, 0))
              .polyline([(SPINE_Y_F, 10.0), (SPINE_Y_F, 17.0), (SPINE_Y_F + 2.5, 19.3),
                         (-12.0, SPINE_TOP), (SPINE_Y_RS + 3.0, SPINE_TOP),
                         (SPINE_Y_RS + 3.0, 10.0)])
              .close().extrude(40.0))
spine = spine_plan.intersect(spine_side)
try:
    spine = spine.edges("|Y").edges(">Z").chamfer(0.5)
except Exception:
    pass

# raised rear deck: flat top, sloping shoulders running out to thin side plates
DECK_TOP = 26.7
DECK_Y1 = 37.7
DECK_TW = 6.0        # half width of flat top
PLATE_W = 10.8       # half width of side plates
PLATE_Z = 24.2
deck_sec = (cq.Workplane("XZ", origin=(0, DECK_Y1, 0))
            .polyline([(-PLATE_W, PLATE_Z - 0.5), (-PLATE_W, PLATE_Z), (-DECK_TW, DECK_TOP),
                       (DECK_TW, DECK_TOP), (PLATE_W, PLATE_Z), (PLATE_W, PLATE_Z - 0.5),
                       (5.0, PLATE_Z - 0.5), (5.0, 18.0), (-5.0, 18.0), (-5.0, PLATE_Z - 0.5)])
            .close().extrude(DECK_Y1 - SPINE_Y_RS))
deck_side = (cq.Workplane("YZ", origin=(-20, 0, 0))
             .polyline([(SPINE_Y_RS, 17.0), (SPINE_Y_RS, SPINE_TOP - 0.4),
                        (SPINE_Y_RS + 3.0, DECK_TOP), (DECK_Y1 - 1.0, DECK_TOP),
                        (DECK_Y1, DECK_TOP - 1.0), (DECK_Y1, 17.0)]).close()
             .extrude(40.0))
deck_plan = (cq.Workplane("XY").workplane(offset=15.0)
             .polyline([(-SPINE_W_R, SPINE_Y_RS), (SPINE_W_R, SPINE_Y_RS),
                        (PLATE_W, SPINE_Y_RS + 2.5), (PLATE_W, 33.0), (8.3, 33.0),
                        (8.3, DECK_Y1), (-8.3, DECK_Y1), (-8.3, 33.0), (-PLATE_W, 33.0),
                        (-PLATE_W, SPINE_Y_RS + 2.5)]).close()
             .extrude(15.0))
deck = deck_sec.intersect(deck_side).intersect(deck_plan)
# centre slot with a small block at its rear end, and a side pocket
deck = deck.cut(cq.Workplane("XY").box(3.6, 21.0, 2.0).translate((0, 26.8, DECK_TOP)))
deck = deck.cut(cq.Workplane("XY").box(3.0, 10.0, 2.0)
                .translate((7.2, 23.5, 0.5 * (DECK_TOP + PLATE_Z) + 0.9)))
deck_tail = cq.Workplane("XY").box(3.0, 5.4, 1.7).translate((0, 33.9, DECK_TOP - 0.3))

# turret pad (stadium, drafted sides) and dome with twin guns
PAD_L, PAD_W = 19.4, 8.4
PAD_YC = -3.8
PAD_TOP = SPINE_TOP + 1.3
pad = (cq.Workplane("XY").workplane(offset=PAD_TOP - 4.0)
       .center(0, PAD_YC).slot2D(PAD_L + 2.2, PAD_W + 2.2, angle=90)
       .extrude(4.0, taper=15))
pad = pad.cut(cq.Workplane("XY").workplane(offset=PAD_TOP - 0.3).center(0, PAD_YC)
              .slot2D(PAD_L - 1.4, PAD_W - 1.6, angle=90).extrude(1.0))
DOME_R = 3.1
DOME_Y = -6.4
dome = cq.Workplane("XY").sphere(DOME_R).translate((0, DOME_Y, PAD_TOP - 0.1))
dome = dome.intersect(cq.Workplane("XY").box(10, 10, 10).translate((0, DOME_Y, PAD_TOP + 4.9)))
dome_ring = (cq.Workplane("XY").workplane(offset=PAD_TOP - 0.4).center(0, DOME_Y)
             .circle(DOME_R + 0.3).extrude(1.0))
guns = cq.Workplane("XY")
for gx in (-0.55, 0.55):
    g = (cq.Workplane("XZ", origin=(gx, DOME_Y + 1.5, PAD_TOP + 1.9)).circle(0.25)
         .extrude(-5.8))
    sl = (cq.Workplane("XZ", origin=(gx, DOME_Y + 5.2, PAD_TOP + 1.9)).circle(0.42)
          .extrude(-2.0))
    guns = guns.union(g).union(sl)
dome = dome.union(dome_ring)

# ---------------- rear deck and big engines ----------------
# thin webs carrying the engines, box between them under the deck
eng_sup = cq.Workplane("XY")
for s in (1, -1):
    eng_sup = eng_sup.union(cq.Workplane("XY").box(1.6, 11.3, 4.6)
                            .translate((s * 7.8, 25.65, 16.2)))
rear_mid = cq.Workplane("XY").box(8.6, 7.0, 7.6).translate((0, 34.2, 20.6))
bumps = cq.Workplane("XY")
for bx, bz in ((-2.4, 21.8), (2.4, 20.4)):
    bumps = bumps.union(cq.Workplane("XZ", origin=(bx, 37.7, bz)).circle(0.65).extrude(-0.6))


def engine(r_body, r_neck, r_noz, y_front, y_body, y_neck, y_full, y_end):
    """Revolved engine: rounded cylinder body, neck, bottle-shaped nozzle."""
    s45 = math.sqrt(0.5)
    dr = r_noz - r_neck
    dy = y_full - y_neck
    w = (cq.Workplane("XY").moveTo(0, y_front - r_body)
         .threePointArc((r_body * s45, y_front - r_body * s45), (r_body, y_front))
         .lineTo(r_body, y_body).lineTo(r_neck, y_body + 0.4).lineTo(r_neck, y_neck)
         .spline([(r_neck + 0.25 * dr, y_neck + 0.3 * dy),
                  (r_neck + 0.75 * dr, y_neck + 0.62 * dy),
                  (r_noz, y_full)], includeCurrent=True)
         .threePointArc((r_noz + 0.12, 0.5 * (y_full + y_end - 1.0)), (r_noz, y_end - 1.0))
         .threePointArc((r_noz - 0.2, y_end - 0.3), (r_noz - 0.6, y_end))
         .lineTo(0, y_end).close())
    solid = w.revolve(360, (0, 0, 0), (0, 1, 0))
    hole = (cq.Workplane("XZ", origin=(0, y_end + 0.01, 0)).circle(r_noz - 0.75)
            .extrude(2.5))
    return solid.cut(hole)


big = engine(3.0, 2.6, 4.0, 16.9, 32.7, 33.6, 41.5, 50.4)
small_e = engine(1.85, 1.55, 2.75, 26.0, 37.0, 37.8, 41.5, 45.4)
engines = cq.Workplane("XY")
for s in (1, -1):
    engines = engines.union(big.translate((s * ENG_X, 0, ENG_Z)))
engines = engines.union(small_e.translate((0, 0, CEN_Z_MID)))
engines = engines.union(small_e.translate((0, 0, CEN_Z_LOW)))

# side pipes along the centre body
pipes = cq.Workplane("XY")
for s in (1, -1):
    pipes = pipes.union(cq.Workplane("XZ", origin=(s * 10.9, 17.5, 21.3))
                        .circle(0.35).extrude(19.0))
    pipes = pipes.union(cq.Workplane("XZ", origin=(s * 10.2, 17.5, 21.25))
                        .circle(0.25).extrude(16.0))

# ---------------- wing-tip pods ----------------
oct_c = POD_R * 0.42
pod_body = (cq.Workplane("YZ", origin=(POD_X0, 0, 0))
            .polyline([(-POD_R + oct_c, -POD_R), (POD_R - oct_c, -POD_R),
                       (POD_R, -POD_R + oct_c), (POD_R, POD_R - oct_c),
                       (POD_R - oct_c, POD_R), (-POD_R + oct_c, POD_R),
                       (-POD_R, POD_R - oct_c), (-POD_R, -POD_R + oct_c)]).close()
            .extrude(POD_X1 - POD_X0))
cap = (cq.Workplane("XY")
       .moveTo(0, 0).lineTo(POD_R - 0.35, 0)
       .threePointArc((POD_R - 0.9, 1.5), (3.3, POD_TIP - POD_X1))
       .lineTo(0, POD_TIP - POD_X1).close()
       .revolve(360, (0, 0, 0), (0, 1, 0)))
# cap axis is Y; rotate so it points along +X
cap = cap.rotate((0, 0, 0), (0, 0, 1), -90).translate((POD_X1, 0, 0))
cap_hole = (cq.Workplane("YZ", origin=(POD_TIP - 0.5, 0, 0)).circle(2.75).extrude(1.0))
pod = pod_body.union(cap).cut(cap_hole).translate((0, Y_BAND_C, Z_MID))
pods = pod.union(pod.mirror("YZ"))

# ---------------- nose: cockpit, chin, mandibles ----------------
# cockpit canopies: lens shapes (two intersecting spheres) giving a centre crease
CAN_LO = (-45.3, 10.5, 5.2, 0.9)    # (y, z, sphere radius, lateral offset)
CAN_HI = (-40.6, 14.4, 4.9, 0.8)


def canopy(cy, cz, rr, off):
    """Lens of two spheres (centres at x = +-off) built as a revolve about X."""
    h = math.sqrt(rr * rr - off * off)
    th = math.atan2(h, -off)
    mid = 0.5 * (math.pi + th)
    p_mid = (off + rr * math.cos(mid), rr * math.sin(mid))
    prof = (cq.Workplane("XY").moveTo(-(rr - off), 0)
            .threePointArc(p_mid, (0, h))
            .threePointArc((-p_mid[0], p_mid[1]), (rr - off, 0))
            .close())
    return prof.revolve(360, (0, 0, 0), (1, 0, 0)).translate((0, cy, cz))


ball_lo = canopy(*CAN_LO)
ball_hi = canopy(*CAN_HI)
chin = cq.Workplane("XY").box(9.6, 9.5, 9.0).translate((0, -39.75, 4.5))
chin_guns = cq.Workplane("XY")
for gx in (-1.2, 1.2):
    chin_guns = chin_guns.union(cq.Workplane("XZ", origin=(gx, -44.4, 5.3))
                                .circle(0.35).extrude(5.0))

PR_Z0, PR_Z1 = 11.1, 13.3    # mandible rails
PR_Y_TIP = -49.2
PR_Y_BACK = -40.0
PR_XI, PR_XO = 5.8, 13.0     # inner / outer faces of a rail pair
RAIL_W = 2.0
prongs = cq.Workplane("XY")
for s in (1, -1):
    zc = 0.5 * (PR_Z0 + PR_Z1)
    for xr in (PR_XI + 0.5 * RAIL_W, PR_XO - 0.5 * RAIL_W):
        rail = cq.Workplane("XY").box(RAIL_W, PR_Y_BACK - PR_Y_TIP, PR_Z1 - PR_Z0).translate(
            (s * xr, 0.5 * (PR_Y_TIP + PR_Y_BACK), zc))
        prongs = prongs.union(rail)
    xm = 0.5 * (PR_XI + PR_XO)
    cross = cq.Workplane("XY").box(PR_XO - PR_XI - 0.2, 2.4, PR_Z1 - PR_Z0 - 0.4).translate(
        (s * xm, -46.4, zc - 0.2))
    frame = cq.Workplane("XY").box(2.8, 3.4, 0.9).translate((s * xm, -43.5, PR_Z1 + 0.3))
    posts = cq.Workplane("XY")
    for dx in (-0.9, 0.9):
        posts = posts.union(cq.Workplane("XY").box(0.5, 3.0, 0.5)
                            .translate((s * (xm + dx), -46.8, PR_Z1 - 0.3)))
    prongs = prongs.union(cross).union(frame).union(posts)

# canopy frame ribs: two hoops round each canopy
ribs = cq.Workplane("XY")
for (cy, cz, rr, off) in (CAN_LO, CAN_HI):
    outer = canopy(cy, cz, rr + 0.2, off)
    inner = canopy(cy, cz, rr - 0.6, off)
    shell = outer.cut(inner)
    for dy in (-0.15 * rr, 0.35 * rr):
        ribs = ribs.union(shell.intersect(
            cq.Workplane("XY").box(3 * rr, 0.4, 3 * rr).translate((0, cy + dy, cz))))

# ---------------- assemble ----------------
result = (wing.union(centre).union(band_up).union(band_lo).union(keel)
          .union(rear_block).union(spine).union(pad).union(dome).union(guns)
          .union(deck).union(deck_tail).union(eng_sup).union(rear_mid)
          .union(bumps).union(engines).union(pipes)
          .union(pods).union(ball_lo).union(ball_hi).union(chin)
          .union(chin_guns).union(prongs).union(ribs))

VIEW = {"azimuth": 45, "elevation": 26}
